import math
import cadquery as cq

# =====================================================================
# Clamping / slider plate with pressed threaded boss
#   body: solid block with bevelled -X and -Y top edges,
#         +X undercut (45 deg) below a thin top plate,
#         +Y wall, underside groove along Y (exits through the +Y wall),
#         threaded boss with counterbore, counterbored plain hole.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
LX = 48.0          # length along X
LY = 37.3          # width along Y
H = 5.34           # overall height of the body (without boss)
T_PLATE = 1.3      # thickness of the top plate over the undercut / groove
H_SIDE = 1.42      # vertical land at the bottom of the -X and -Y sides

# -X bevel (45 deg)
BEV_X = H - H_SIDE                      # horizontal width of the -X bevel
# -Y bevel (steeper, ~56 deg)
BEV_Y = 2.64                            # horizontal width of the -Y bevel
BEV_Y_X0 = 36.0                         # end of bevel at its lower edge
BEV_Y_X1 = 38.9                         # end of bevel at its upper edge
BEV_Y_X2 = 41.5                         # end of the run-out face on the -Y edge

CORNER_CH = 4.06   # plan chamfer at the +X/-Y corner
EDGE_CH = 0.3      # small chamfer on the top edges at +X end

# +X undercut (45 deg) below the top plate, bounded by +Y wall
UC_X0 = 40.1       # x of undercut at z = 0
WALL_Y = 1.83      # thickness of the +Y wall (not undercut)

# groove on the underside along Y near -X side (exits through +Y wall)
GR_X0 = 6.6
GR_X1 = 18.7
GR_Y0 = 2.85
GR_CH_M = 1.1      # chamfer at -X top corner of groove
GR_CH_P = 1.3      # chamfer at +X top corner of groove

# boss with threaded hole
BOSS_X, BOSS_Y = 29.8, 14.6
BOSS_D = 13.3
BOSS_H = 4.6
BOSS_CH = 0.45         # outer top chamfer
BOSS_CB_D = 10.6       # counterbore diameter
BOSS_CB_CH = 0.45      # chamfer on counterbore edge
BOSS_CB_DEPTH = 1.7    # counterbore depth (from boss top)
BOSS_CSK_D = 7.4       # countersink entry diameter (on counterbore floor)
BOSS_CSK_ANGLE = 120.0 # countersink included angle
THREAD_D = 4.1         # thread minor diameter
THREAD_MAJ_D = 5.0     # thread major diameter
THREAD_P = 0.8         # thread pitch (rings)
BOT_BORE_D = 5.5       # plain bore from the underside
BOT_BORE_DEPTH = 3.0

# plain counterbored hole
HOLE_X, HOLE_Y = 29.6, 27.9
HOLE_CB_D = 8.6
HOLE_CB_CH = 0.25
HOLE_CB_DEPTH = 4.3
HOLE_D = 4.6
HOLE_BOT_CH = 0.33

SEAM_ANGLE = 45.0      # rotate round features so seams sit on silhouettes
SEAM_ANGLE_BORE = -45.0  # seam of bores on the near (hidden) side

zt = H - T_PLATE       # underside of the top plate

# ---------------- base block ----------------
body = cq.Workplane("XY").box(LX, LY, H, centered=False)

# -X bevel: remove everything above plane z = H_SIDE + x
bx = (
    cq.Workplane("XZ")
    .polyline([(-1, H_SIDE - 1), (BEV_X + 1, H + 1), (-1, H + 1)])
    .close()
    .extrude(-(LY + 2))
    .translate((0, -1, 0))
)
body = body.cut(bx)

# -Y bevel wedge with a planar run-out end face
tan_y = (H - H_SIDE) / BEV_Y
wedge = (
    cq.Workplane("YZ")
    .polyline([(-1, H_SIDE - tan_y), (BEV_Y + 1.0 / tan_y, H + 1), (-1, H + 1)])
    .close()
    .extrude(LX)
    .translate((-1, 0, 0))
)
P0 = cq.Vector(BEV_Y_X0, 0, H_SIDE)
P1 = cq.Vector(BEV_Y_X1, BEV_Y, H)
P2 = cq.Vector(BEV_Y_X2, 0, H)
n = (P1 - P0).cross(P2 - P0).normalized()
if n.x < 0:
    n = -n
half = cq.Workplane(cq.Plane(origin=P0, xDir=(P2 - P0).normalized(), normal=n)).rect(200, 200).extrude(100)
wedge = wedge.cut(half)
body = body.cut(wedge)

# plan chamfer at +X/-Y corner (line through (LX-CH,0) and (LX,CH))
cc = (
    cq.Workplane("XY")
    .polyline([(LX - CORNER_CH - 1, -1), (LX + 1, -1), (LX + 1, CORNER_CH + 1)])
    .close()
    .extrude(H + 2)
    .translate((0, 0, -1))
)
body = body.cut(cc)

# small chamfer along the top edges of the +X end, the corner chamfer and
# the short straight -Y edge next to it
def _top_end_edges(b):
    sel = []
    for e in b.edges().vals():
        p0, p1 = e.startPoint(), e.endPoint()
        if abs(p0.z - H) > 1e-4 or abs(p1.z - H) > 1e-4:
            continue
        xm = 0.5 * (p0.x + p1.x)
        ym = 0.5 * (p0.y + p1.y)
        if abs(p0.x - LX) < 1e-4 and abs(p1.x - LX) < 1e-4:
            sel.append(e)  # +X top edge
        elif xm > LX - CORNER_CH - 1e-3 and ym < CORNER_CH + 1e-3 and abs(p0.x - p1.x) > 1e-3 and abs(p0.y - p1.y) > 1e-3:
            sel.append(e)  # corner chamfer top edge
        elif abs(p0.y) < 1e-4 and abs(p1.y) < 1e-4 and xm > BEV_Y_X2 - 1e-3:
            sel.append(e)  # short -Y edge
    return sel

body = body.newObject(_top_end_edges(body)).chamfer(EDGE_CH)

# +X undercut under the top plate
uc = (
    cq.Workplane("XZ")
    .polyline([(UC_X0 - 1, -1), (LX + 1, -1), (LX + 1, zt), (UC_X0 + zt, zt)])
    .close()
    .extrude(-(LY - WALL_Y + 1))
    .translate((0, -1, 0))
)
body = body.cut(uc)

# underside groove along Y (exits through +Y wall), chamfered top corners
gr = (
    cq.Workplane("XZ")
    .polyline(
        [
            (GR_X0, -1),
            (GR_X1, -1),
            (GR_X1, zt - GR_CH_P),
            (GR_X1 - GR_CH_P, zt),
            (GR_X0 + GR_CH_M, zt),
            (GR_X0, zt - GR_CH_M),
        ]
    )
    .close()
    .extrude(-(LY - GR_Y0 + 1))
    .translate((0, GR_Y0, 0))
)
body = body.cut(gr)


def revolved(profile, cx, cy, seam=SEAM_ANGLE):
    """Revolve an (r, z) profile about the vertical axis through (cx, cy)."""
    s = (
        cq.Workplane("XZ")
        .polyline(profile)
        .close()
        .revolve(360, (0, 0, 0), (0, 1, 0))
        .rotate((0, 0, 0), (0, 0, 1), seam)
        .translate((cx, cy, 0))
    )
    return s


# boss (chamfered top outer edge)
ztop = H + BOSS_H
rb = BOSS_D / 2
boss = revolved(
    [(0, H - 0.5), (rb, H - 0.5), (rb, ztop - BOSS_CH), (rb - BOSS_CH, ztop), (0, ztop)],
    BOSS_X,
    BOSS_Y,
)
body = body.union(boss)

# boss bore: chamfered counterbore, countersink, thread (modelled as plain
# V-rings between minor and major diameter), underside bore
rcb = BOSS_CB_D / 2
rcs = BOSS_CSK_D / 2
rmaj = THREAD_MAJ_D / 2
rmin = THREAD_D / 2
rbb = BOT_BORE_D / 2
zfl = ztop - BOSS_CB_DEPTH
zth = zfl - (rcs - rmaj) * math.tan(math.radians(90 - BOSS_CSK_ANGLE / 2))  # start of thread
n_rings = int((zth - BOT_BORE_DEPTH) / THREAD_P)
prof = [
    (0, ztop + 1),
    (rcb + BOSS_CB_CH + 1, ztop + 1),
    (rcb, ztop - BOSS_CB_CH),
    (rcb, zfl),
    (rcs, zfl),
    (rmaj, zth),
]
z = zth
for i in range(n_rings):
    prof.append((rmin, z - THREAD_P / 2))
    z -= THREAD_P
    if i < n_rings - 1:
        prof.append((rmaj, z))
prof += [(rmin, BOT_BORE_DEPTH), (rbb, BOT_BORE_DEPTH), (rbb, -1), (0, -1)]
bore = revolved(prof, BOSS_X, BOSS_Y, SEAM_ANGLE_BORE)
body = body.cut(bore)

# plain counterbored hole (chamfered top edge and bottom edge)
rh = HOLE_CB_D / 2
rs = HOLE_D / 2
hole = revolved(
    [
        (0, H + 1),
        (rh + HOLE_CB_CH + 1, H + 1),
        (rh, H - HOLE_CB_CH),
        (rh, H - HOLE_CB_DEPTH),
        (rs, H - HOLE_CB_DEPTH),
        (rs, HOLE_BOT_CH),
        (rs + HOLE_BOT_CH + 1, -1),
        (0, -1),
    ],
    HOLE_X,
    HOLE_Y,
    SEAM_ANGLE_BORE,
)
body = body.cut(hole)

result = body
